import math
import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
LENGTH = 80.0          # overall length (X), tip to tip of the round ends
WIDTH = 52.0           # overall width (Y), across the two flat sides
HEIGHT = 21.0          # overall height (Z)
END_R = 31.0           # radius of the two round ends (plan view)
CORNER_R = 9.0         # blend radius between flat sides and round ends

DISH_D = 36.0          # spherical dish diameter at the top face
DISH_SPHERE_R = 20.0   # radius of the ball that forms the dish

HOLE_PITCH = 66.0      # centre distance of the two end holes
HOLE_D = 4.4           # end hole diameter (through)
CENTER_HOLE_D = 4.4    # centre hole diameter (through, from dish bottom)

# ---------------- plan-view outline ----------------
h = WIDTH / 2.0
c = LENGTH / 2.0 - END_R                      # x of the end-arc centres
# corner blend: circle of CORNER_R tangent to flat y=h and inside the end arc
xf = c + math.sqrt((END_R - CORNER_R) ** 2 - (h - CORNER_R) ** 2)
yf = h - CORNER_R
ux, uy = (xf - c) / (END_R - CORNER_R), yf / (END_R - CORNER_R)
xt, yt = c + END_R * ux, END_R * uy           # blend / end-arc tangent point


def blend_mid(sx, sy):
    """midpoint of the corner blend arc in quadrant (sx, sy)"""
    a0 = math.atan2(1.0, 0.0)                  # tangent on the flat: straight up
    a1 = math.atan2(uy, ux)                    # tangent on the end arc
    am = 0.5 * (a0 + a1)
    return (sx * (xf + CORNER_R * math.cos(am)), sy * (yf + CORNER_R * math.sin(am)))


outline = (
    cq.Workplane("XY")
    .moveTo(-xf, h)
    .lineTo(xf, h)
    .threePointArc(blend_mid(1, 1), (xt, yt))
    .threePointArc((LENGTH / 2.0, 0.0), (xt, -yt))
    .threePointArc(blend_mid(1, -1), (xf, -h))
    .lineTo(-xf, -h)
    .threePointArc(blend_mid(-1, -1), (-xt, -yt))
    .threePointArc((-LENGTH / 2.0, 0.0), (-xt, yt))
    .threePointArc(blend_mid(-1, 1), (-xf, h))
    .close()
)
body = outline.extrude(HEIGHT)

# ---------------- spherical dish ----------------
a = DISH_D / 2.0
sph_r = DISH_SPHERE_R
dish_depth = sph_r - math.sqrt(sph_r ** 2 - a ** 2)   # ~11.3 mm
sph_c = HEIGHT - dish_depth + sph_r
# sphere axis laid along X (seam meridian ends up above the part, out of the dish)
sphere = (
    cq.Workplane("XY")
    .add(cq.Solid.makeSphere(sph_r, angleDegrees1=-90, angleDegrees2=90))
    .rotate((0, 0, 0), (0, 1, 0), -90)
    .translate((0, 0, sph_c))
)
body = body.cut(sphere)

# ---------------- through holes ----------------
# two fixing holes in the ends and one small drain/vent hole at the bottom of the dish
body = (
    body.faces(">Z").workplane(centerOption="ProjectedOrigin")
    .pushPoints([(-HOLE_PITCH / 2.0, 0.0), (HOLE_PITCH / 2.0, 0.0)])
    .hole(HOLE_D)
)
body = (
    body.faces("<Z").workplane(centerOption="ProjectedOrigin")
    .hole(CENTER_HOLE_D)
)

result = body

VIEW = {"azimuth": 45, "elevation": 26}
